import math
import cadquery as cq

# ---------------------------------------------------------------------------
# Print plate of small toy parts.  All layout dimensions are given in "grid
# units" (u) measured on the plan view and converted to millimetres by S.
# ---------------------------------------------------------------------------
S = 0.5                    # mm per grid unit (overall plate ~114 x 119 mm)
X0, Y0 = 130.1, 389.9      # plan-view origin (grid units)

T_BAR = 4.0                # thickness of the flat levers / frames
CUBE = 29.3                # letter cube edge
ENGRAVE = 1.2              # letter engraving depth
CLIP_H = 49.7              # tall clip height
FORK_H = 48.8              # tall fork height
WALL_H = 23.0              # L-wall height
HUB_H = 23.0               # hub height of the big gear lever
FOOT_H = 11.0              # height of the arm feet


def P(px, py):
    return ((px - X0) * S, (Y0 - py) * S)


def prism(pts, z0, z1):
    pm = [P(x, y) for x, y in pts]
    return (cq.Workplane("XY").workplane(offset=z0 * S)
            .polyline(pm).close().extrude((z1 - z0) * S))


def box(x0, y0, x1, y1, z0, z1):
    return prism([(x0, y0), (x1, y0), (x1, y1), (x0, y1)], z0, z1)


def cylz(cx, cy, r, z0, z1):
    x, y = P(cx, cy)
    return (cq.Workplane("XY").workplane(offset=z0 * S)
            .center(x, y).circle(r * S).extrude((z1 - z0) * S))


def cylx(x0, x1, cy, cz, r):
    x, y = P(x0, cy)
    return (cq.Workplane("YZ").workplane(offset=x)
            .center(y, cz * S).circle(r * S).extrude((x1 - x0) * S))


def cyly(y0, y1, cx, cz, r):
    # cylinder along world Y between plan rows y0 (back) and y1 (front)
    xa, ya = P(cx, y1)
    _, yb = P(cx, y0)
    return (cq.Workplane("XZ").workplane(offset=-yb)
            .center(xa, cz * S).circle(r * S).extrude(yb - ya))


def rot_pts(pts, ang_deg, cx, cy):
    a = math.radians(ang_deg)
    c, s = math.cos(a), math.sin(a)
    out = []
    for x, y in pts:
        dx, dy = x - cx, y - cy
        out.append((cx + dx * c - dy * s, cy + dx * s + dy * c))
    return out


# ---------------------------------------------------------------------------
# Letters (engraved) -- strokes defined in a unit square, u right, v up
# ---------------------------------------------------------------------------
W = 0.10


def _rect(u0, v0, u1, v1):
    return ("poly", [(u0, v0), (u1, v0), (u1, v1), (u0, v1)])


def _bar(p0, p1, w):
    (x0, y0), (x1, y1) = p0, p1
    L = math.hypot(x1 - x0, y1 - y0)
    nx, ny = -(y1 - y0) / L * w / 2, (x1 - x0) / L * w / 2
    return ("poly", [(x0 + nx, y0 + ny), (x1 + nx, y1 + ny), (x1 - nx, y1 - ny), (x0 - nx, y0 - ny)])


LETTERS = {
    "E": [_rect(0.22, 0.1, 0.22 + W, 0.9), _rect(0.22, 0.1, 0.78, 0.1 + W),
          _rect(0.22, 0.5 - W / 2, 0.72, 0.5 + W / 2), _rect(0.22, 0.9 - W, 0.78, 0.9)],
    "R": [_rect(0.2, 0.1, 0.2 + W, 0.9), _rect(0.2, 0.9 - W, 0.55, 0.9),
          _rect(0.2, 0.45, 0.55, 0.45 + W),
          ("ring", 0.55, 0.675, 0.225, 0.225 - W),
          _bar((0.45, 0.48), (0.8, 0.1), W)],
    "A": [_bar((0.14, 0.1), (0.5, 0.9), W), _bar((0.86, 0.1), (0.5, 0.9), W),
          _rect(0.3, 0.33, 0.7, 0.33 + W)],
}


def letter_solid(ch, size, rot):
    """Letter cutter in local frame: centred, face plane z=0, cutting into -z."""
    res = None
    z0, hz = -ENGRAVE * S, (ENGRAVE + 1.0) * S
    for item in LETTERS[ch]:
        if item[0] == "poly":
            pts = [((u - 0.5) * size, (v - 0.5) * size) for u, v in item[1]]
            pts = rot_pts(pts, rot, 0.0, 0.0)
            s = cq.Workplane("XY").workplane(offset=z0).polyline(pts).close().extrude(hz)
        else:
            _, cu, cv, ro, ri = item
            c = ((cu - 0.5) * size, (cv - 0.5) * size)
            ring = (cq.Workplane("XY").workplane(offset=z0).center(*c)
                    .circle(ro * size).circle(ri * size).extrude(hz))
            half = (cq.Workplane("XY").workplane(offset=z0 - 0.1)
                    .center(c[0] + ro * size / 2, c[1]).rect(ro * size, 2.2 * ro * size)
                    .extrude(hz + 0.2))
            s = ring.intersect(half).rotate((0, 0, 0), (0, 0, 1), rot)
        res = s if res is None else res.union(s)
    return res


def place_on_face(w, face, c, a):
    cx, cy, cz = c
    if face == "top":
        return w.translate((cx, cy, cz + a))
    if face == "bottom":
        return w.rotate((0, 0, 0), (1, 0, 0), 180).translate((cx, cy, cz - a))
    w = w.rotate((0, 0, 0), (1, 0, 0), 90)
    if face == "front":
        return w.translate((cx, cy - a, cz))
    if face == "right":
        return w.rotate((0, 0, 0), (0, 0, 1), 90).translate((cx + a, cy, cz))
    if face == "back":
        return w.rotate((0, 0, 0), (0, 0, 1), 180).translate((cx, cy + a, cz))
    if face == "left":
        return w.rotate((0, 0, 0), (0, 0, 1), -90).translate((cx - a, cy, cz))
    raise ValueError(face)


def letter_cube(x0, y0, faces):
    x1, y1 = x0 + CUBE, y0 + CUBE
    cube = box(x0, y0, x1, y1, 0, CUBE)
    cx, cy = P((x0 + x1) / 2, (y0 + y1) / 2)
    a = CUBE * S / 2
    for face, ch, rot in faces:
        cut = place_on_face(letter_solid(ch, CUBE * S * 0.86, rot), face, (cx, cy, a), a)
        cube = cube.cut(cut)
    return cube


# ---------------------------------------------------------------------------
# Parts
# ---------------------------------------------------------------------------

def part_twist_key():
    """Flat key that twists up into a vertical fin with a cross tip."""
    t0, t1 = 3.0, 4.6
    bar = box(20.4, 271.0, 86.5, 294.0, 0, t1).edges("|Z").edges("<X").fillet(8 * S)
    # cross groove pattern + hole
    bar = bar.cut(box(40.2, 270, 44.8, 295, t0, t1 + 1))
    # (grooves are 1.6 deep)
    bar = bar.cut(prism([(18.0, 279.6), (42.5, 278.8), (42.5, 286.1), (18.0, 285.3)], t0, t1 + 1))
    bar = bar.cut(prism([(42.5, 277.6), (64.0, 279.6), (64.0, 285.4), (42.5, 286.9)], t0, t1 + 1))
    bar = bar.cut(cylz(64.0, 282.5, 2.9, t0, t1 + 1))
    bar = bar.cut(cylz(42.5, 282.5, 3.5, -1, t1 + 1))
    # twisted transition: the strip turns 90 deg about X while lifting so it
    # stays on the bed, ending as a vertical fin
    half_w = 11.5
    _, yc = P(0, 282.5)
    wires = []
    for i, (px, ang) in enumerate(((86.0, 0.0), (93.0, 30.0), (100.0, 60.0), (106.5, 90.0))):
        half_t = t1 / 2 + (1.5 - t1 / 2) * i / 3.0
        xw, _ = P(px, 0)
        a = math.radians(ang)
        zc = half_w * math.sin(a) + half_t * math.cos(a)
        pts = []
        for (dy, dz) in ((-half_w, -half_t), (half_w, -half_t), (half_w, half_t), (-half_w, half_t)):
            ry = dy * math.cos(a) - dz * math.sin(a)
            rz = dy * math.sin(a) + dz * math.cos(a)
            pts.append(cq.Vector(xw, yc + ry * S, (zc + rz) * S))
        wires.append(cq.Wire.makePolygon(pts, close=True))
    twist = cq.Workplane("XY").add(cq.Solid.makeLoft(wires, False))
    fin = box(106.0, 281.0, 118.0, 284.0, 0, 23)
    tip = box(112.0, 276.4, 115.0, 288.6, 0, 23)
    return bar.union(twist).union(fin).union(tip)


def part_window_key():
    """Flat key: thick end with a window, S-curved step, thin cross-grooved end."""
    tl, tr = 7.7, 4.0
    outline = [(25.4, 299.3), (73.0, 299.3), (77.0, 301.4), (150.0, 301.4), (150.0, 324.1),
               (77.0, 324.1), (73.0, 326.6), (25.4, 326.6), (22.4, 323.6), (22.4, 302.3)]
    body = prism(outline, 0, tl)
    body = body.union(box(148.0, 301.4, 157.0, 324.1, 0, tl).edges("|Z").edges(">X").fillet(7 * S))
    # S-curved thickness step (cut away everything above the profile)
    xa, _ = P(76.0, 0)
    xb, _ = P(106.5, 0)
    xc, _ = P(160.0, 0)
    _, y0 = P(0, 330)
    _, y1 = P(0, 296)
    prof = (cq.Workplane("XZ").moveTo(xa, tl * S)
            .spline([(xb, tr * S)], tangents=[(1, 0), (1, 0)], includeCurrent=True)
            .lineTo(xc, tr * S).lineTo(xc, 12 * S).lineTo(xa, 12 * S).close()
            .extrude(-(y1 - y0)).translate((0, y0, 0)))
    body = body.cut(prof)
    body = body.cut(box(33.2, 304.3, 62.8, 320.9, -1, tl + 1))
    # cross groove pattern around the hole
    g0 = tr - 1.5
    body = body.cut(box(132.3, 300, 136.6, 326, g0, tl))
    body = body.cut(prism([(110.0, 309.9), (134.2, 307.6), (134.2, 318.0), (110.0, 315.7)], g0, tl))
    body = body.cut(cylz(110.0, 312.8, 2.9, g0, tl))
    body = body.cut(prism([(134.2, 309.1), (158.0, 310.0), (158.0, 315.6), (134.2, 316.5)], g0, tl))
    body = body.cut(cylz(134.2, 313.0, 3.5, -1, tl + 1))
    return body


def part_tall_clip():
    """Standing fork clip: two gamma-shaped plates (slightly tapered) joined by a web."""
    def gamma(p_out_l, p_out_r, p_in_l, p_in_r):
        plan = [(128.0, p_out_l), (155.7, p_out_r), (155.7, p_in_r), (128.0, p_in_l)]
        top = prism(plan, CLIP_H - 10.2, CLIP_H)
        post = prism([(147.0, p_out_r), (155.7, p_out_r), (155.7, p_in_r), (147.0, p_in_r)], 0, CLIP_H)
        return top.union(post)
    web = box(152.3, 277.4, 155.7, 293.3, 0, CLIP_H)
    back = gamma(278.6, 277.4, 281.0, 281.4)
    front = gamma(292.2, 293.3, 289.4, 289.7)
    return back.union(front).union(web)


def part_u_frame():
    """Low U frame with a taller back rail."""
    back = box(163.7, 276.5, 209.3, 282.0, 0, 20)
    front = box(163.7, 300.5, 209.3, 308.0, 0, 19)
    front = front.cut(box(205.0, 300, 210, 303.5, 14, 20))
    close = box(163.7, 276.5, 168.5, 308.0, 0, 19)
    return back.union(front).union(close)


def part_cradle_box():
    """Small cradle: floor with window, slotted front/back walls, pin sideways."""
    h = 20.0
    b = box(211.0, 282.1, 237.0, 323.3, 0, h)
    b = b.union(box(209.8, 312.1, 212.0, 323.3, 0, h))
    b = b.cut(box(215.5, 287.0, 238.0, 318.4, 5, h + 1))
    b = b.cut(box(210.5, 287.0, 216.0, 312.0, 12.5, h + 1))
    b = b.cut(box(220.2, 290.2, 226.6, 315.0, -1, 6))
    b = b.cut(box(222.5, 281, 227.5, 288, 8, h + 1))
    b = b.cut(box(222.5, 317, 227.5, 324.5, 8, h + 1))
    # chamfered outer ends of the walls
    xa, _ = P(230.5, 0)
    xb, _ = P(238.0, 0)
    ch = (cq.Workplane("XZ").polyline([(xa, h * S + 0.1), (xb + 0.1, h * S + 0.1), (xb + 0.1, 11.5 * S)])
          .close().extrude(-40).translate((0, P(0, 330)[1], 0)))
    b = b.cut(ch)
    pin = cylx(192.3, 212.0, 291.5, 10.5, 4.0)
    return b.union(pin)


def part_tall_fork():
    """Tall fork: two slotted flexure plates, a solid block and a notched back bar."""
    f = box(162.4, 318.3, 203.5, 337.8, 0, FORK_H)
    # the middle block stands a little lower than the plates
    f = f.cut(box(186.6, 322.7, 197.2, 339, 44.4, FORK_H + 1))
    # rounded notch across the back bar (seen from the front)
    notch = cyly(317, 339, 177.7, 42.6, 9.5).union(box(168.2, 317, 187.2, 339, 42.6, FORK_H + 1))
    notch = notch.intersect(box(168.6, 316, 197.2, 340, 0, FORK_H + 2))
    f = f.cut(notch)
    # open pocket from the front above a low slab with a U cut-out
    f = f.cut(box(168.6, 322.7, 186.6, 339, 6, FORK_H + 1))
    f = f.cut(box(168.6, 331.5, 186.6, 339, -1, 7))
    f = f.cut(cylz(177.6, 331.5, 8.8, -1, 7))
    # vertical slots in the side plates
    f = f.cut(box(161, 328.2, 169.0, 333.2, 33.5, FORK_H + 1))
    f = f.cut(box(197.0, 328.2, 204.5, 333.2, 33.5, FORK_H + 1))
    # thin slit between the block and the right plate
    f = f.cut(box(197.2, 322.7, 197.9, 339, 15, FORK_H + 1))
    # horizontal flexure slits
    f = f.cut(box(161, 323.9, 168.6, 339, 23, 27))
    f = f.cut(box(161, 323.9, 204.5, 339, 10, 14))
    return f


def arm_part(mirror_xy, ox, oy):
    """Long arm with a polygonal head and an angled foot (pocketed)."""
    head = [(21.5, 331.7), (37.4, 330.3), (43.2, 335.6), (44.6, 346.2), (39.8, 353.8),
            (39.8, 457.5), (64.8, 495.2), (50.0, 505.3), (23.7, 460.2), (24.4, 356.7),
            (17.7, 350.0), (16.7, 339.4)]
    # foot on the angled end: bottom outline and (inset) top outline
    foot_bot = [(27.5, 466.6), (42.5, 461.3), (64.8, 495.2), (50.0, 505.3)]
    ridge = [(34.5, 468.3), (39.9, 465.6), (56.7, 493.8), (52.0, 496.3)]

    def tf(pts):
        out = []
        for x, y in pts:
            if mirror_xy:
                x, y = y - 330.3, x - 16.7
            else:
                x, y = x - 16.7, y - 330.3
            out.append((x + ox, y + oy))
        if mirror_xy:
            out = out[::-1]
        return out

    body = prism(tf(head), 0, T_BAR)
    # foot: a block with sloped outer side
    # sloped plinth carrying a narrow ridge block
    wb = cq.Wire.makePolygon([cq.Vector(*P(x, y), 0) for x, y in tf(foot_bot)], close=True)
    wt = cq.Wire.makePolygon([cq.Vector(*P(x, y), 5.5 * S) for x, y in tf(ridge)], close=True)
    f = cq.Workplane("XY").add(cq.Solid.makeLoft([wb, wt], True))
    f = f.union(prism(tf(ridge), 0, FOOT_H))
    return body.union(f)


def part_frame():
    """Central flat frame with windows, raised ends and a cross lever."""
    t_mid, t_end = 5.0, 10.5
    outline = [(48.6, 345.0), (80.2, 345.0), (80.2, 330.7), (135.6, 330.7), (135.6, 345.0),
               (167.8, 345.0), (167.8, 389.6), (48.6, 389.6)]
    f = prism(outline, 0, t_mid)
    f = f.union(box(48.6, 345.0, 70.5, 389.6, 0, t_end))
    f = f.union(box(145.5, 345.0, 167.8, 389.6, 0, t_end))
    # ramps between the levels
    for (xa, xb) in ((70.5, 74.5), (145.5, 141.5)):
        pa, _ = P(xa, 0)
        pb, _ = P(xb, 0)
        _, y0 = P(0, 389.6)
        _, y1 = P(0, 345.0)
        r = (cq.Workplane("XZ").polyline([(pa, t_end * S), (pb, t_mid * S), (pb, 0), (pa, 0)]).close()
             .extrude(-(y1 - y0)).translate((0, y0, 0)))
        f = f.union(r)
    for (x0, y0, x1, y1) in [(52.9, 351.2, 60.5, 384.7), (63.8, 352.8, 82.6, 379.0),
                             (85.9, 351.2, 101.5, 378.2), (114.6, 351.2, 130.2, 378.2),
                             (133.5, 352.8, 152.3, 379.0), (155.6, 351.2, 163.7, 384.7),
                             (85.1, 335.6, 101.5, 343.0), (114.6, 335.6, 130.2, 343.0)]:
        f = f.cut(box(x0, y0, x1, y1, -1, t_end + 1))
    # cross lever
    tab = box(101.3, 385.0, 114.5, 408.0, 0, t_mid).edges("|Z").edges("<Y").fillet(2.5 * S)
    cross = (prism([(105.2, 360.0), (106.2, 358.8), (109.4, 358.8), (110.4, 360.0), (112.8, 382.3),
                    (110.4, 404.5), (109.4, 405.8), (106.2, 405.8), (105.2, 404.5), (102.8, 382.3)],
                   0, t_mid + 1.5)
             .union(box(97.0, 379.8, 118.6, 385.2, 0, t_mid + 1.5).edges("|Z").fillet(2.4 * S)))
    f = f.union(tab).union(cross).cut(cylz(107.8, 382.3, 3.2, -1, t_end))
    return f


def part_l_wall():
    """Two tall walls in an L on a partial floor with a lower front wall."""
    base = prism([(48.4, 413.3), (87.4, 413.3), (87.4, 420.7), (99.5, 420.7), (99.5, 445.8),
                  (48.4, 445.8)], 0, 3)
    ledge = box(48.4, 392.4, 57.8, 445.8, 0, 3)
    wl = box(48.4, 392.4, 52.4, 445.8, 0, WALL_H)
    wb = box(48.4, 392.4, 94.5, 396.5, 0, WALL_H)
    walls = wl.union(wb)
    # rounded inside corner between the two tall walls
    cx, cy = P(52.4, 396.5)
    walls = walls.edges(cq.selectors.NearestToPointSelector((cx, cy, WALL_H * S / 2))).fillet(3.0 * S)
    wf = box(93.5, 420.7, 99.5, 445.8, 0, WALL_H)
    return base.union(ledge).union(walls).union(wf)


def gear_teeth(cx, cy, r_root, r_tip, n, z0, z1, tw, phase=0.0):
    """Spur gear: core cylinder plus n straight teeth with rounded tips."""
    g = cylz(cx, cy, r_root, z0, z1)
    r_c = r_tip - tw / 2
    for i in range(n):
        a = phase + 360.0 / n * i
        pts = [(cx + r_root - 1.0, cy - tw / 2), (cx + r_c, cy - tw / 2),
               (cx + r_c, cy + tw / 2), (cx + r_root - 1.0, cy + tw / 2)]
        g = g.union(prism(rot_pts(pts, a, cx, cy), z0, z1))
        (tx, ty), = rot_pts([(cx + r_c, cy)], a, cx, cy)
        g = g.union(cylz(tx, ty, tw / 2, z0, z1))
    return g


def part_small_gear_lever():
    """Small 8-tooth gear on a short spigot with a lever arm reaching to the bed."""
    cx, cy = 129.4, 407.5
    base = cylz(cx, cy, 4.5, 0, 6)
    top_z = 16.5
    gear = gear_teeth(cx, cy, 7.3, 10.6, 8, 6, top_z, 3.4, 22.5)
    # lever arm sloping from the gear down to the bed
    arm = prism([(133, 399.4), (176, 399.4), (179.5, 401.0), (181.25, 404.0), (180.0, 407.5),
                 (171.25, 407.5), (165, 404.4), (146.25, 404.4), (140, 408.1), (133, 408.1)],
                -1, 14)
    xa, _ = P(133.0, 0)
    xb, _ = P(137.0, 0)
    xc, _ = P(172.0, 0)
    xd, _ = P(182.0, 0)
    side = (cq.Workplane("XZ").polyline([(xa, 7.0 * S), (xa, 12.5 * S), (xb, 12.5 * S), (xd, 5.0 * S),
                                          (xd, 0), (xc, 0)]).close()
            .extrude(-20).translate((0, P(0, 420)[1], 0)))
    arm = arm.intersect(side)
    g = base.union(gear).union(arm)
    # cross pattern of notches in the top face
    for a in (0, 90, 180, 270):
        pts = rot_pts([(cx + 5.0, cy - 1.6), (cx + 8.0, cy - 1.6), (cx + 8.0, cy + 1.6), (cx + 5.0, cy + 1.6)],
                      a, cx, cy)
        g = g.cut(prism(pts, top_z - 2.5, top_z + 1))
    return g.cut(cylz(cx, cy, 3.5, -1, 20))


def part_big_gear_lever():
    """Tall hub with a ring of teeth on a flange and a cantilevered lever arm."""
    cx, cy = 121.25, 436.25
    flange = cylz(cx, cy, 13.75, 0, 2.5)
    gear = gear_teeth(cx, cy, 7.3, 10.6, 8, 2.5, 12, 2.6, 90.0)
    hub = cylz(cx, cy, 7.3, 0, HUB_H)
    arm = prism([(125, 428.1), (170.0, 428.1), (172.5, 429.5), (173.75, 432.5), (172.0, 436.9),
                 (165.0, 436.9), (160.0, 433.1), (137.5, 433.1), (131.0, 437.0), (125, 437.0)],
                HUB_H - 9, HUB_H)
    g = flange.union(gear).union(hub).union(arm)
    return g.cut(cylz(cx, cy, 4.8, -1, HUB_H + 1))


def part_slide_frame():
    """Rectangular frame with ramped rails, wedge back bar and saddle front bar."""
    x0, x1 = 187.6, 243.5
    yb, yf = 343.1, 450.9
    hi, lo = 11.0, 4.0
    fr = box(x0, yb, x1, yf, 0, lo)
    fr = fr.cut(box(199.6, 356.9, 231.3, 419.3, -1, lo + 1))
    fr = fr.cut(prism([(199.6, 419.2), (231.3, 419.2), (222.7, 428.5), (208.9, 428.5)], -1, lo + 1))
    fr = fr.cut(box(208.9, 428.4, 222.7, 442.4, -1, hi + 1))

    # side profile (world YZ) of rails: high back, ramp down, low, ramp up to post
    def yz(py):
        return P(0, py)[1]
    prof = [(yz(343.1), 0), (yz(343.1), hi * S), (yz(347.4), hi * S), (yz(356.6), lo * S),
            (yz(368.7), lo * S), (yz(380.8), hi * S), (yz(389.5), hi * S), (yz(389.5), 0)]
    for (xa, xb) in ((187.6, 199.6), (231.3, 243.5)):
        pa, _ = P(xa, 0)
        pb, _ = P(xb, 0)
        rail = (cq.Workplane("YZ").workplane(offset=pa).polyline(prof).close()
                .extrude(pb - pa))
        fr = fr.union(rail)
    # back wedge bar
    fr = fr.union(box(x0, 343.1, x1, 347.4, 0, hi))
    pa, _ = P(x0, 0)
    pb, _ = P(x1, 0)
    wedge = (cq.Workplane("YZ").workplane(offset=pa)
             .polyline([(yz(347.4), 0), (yz(347.4), hi * S), (yz(356.9), lo * S), (yz(356.9), 0)])
             .close().extrude(pb - pa))
    fr = fr.union(wedge)
    # saddle front bar
    # front bar: concave ramp rising from the front edge to the back edge
    pa, _ = P(x0, 0)
    pb, _ = P(x1, 0)
    front = (cq.Workplane("YZ").workplane(offset=pa)
             .moveTo(yz(yf), 0).lineTo(yz(yf), (hi - 1.0) * S)
             .threePointArc((yz(441.5), (hi - 2.2) * S), (yz(432.0), hi * S))
             .lineTo(yz(432.0), 0).close().extrude(pb - pa))
    front = front.cut(box(208.9, 428.4, 222.7, 442.4, -1, hi + 1))
    fr = fr.union(front)
    # little feet in front
    fr = fr.cut(box(x0 - 1, 447.0, x1 + 1, yf + 1, -1, 4.5))
    fr = fr.union(box(192.0, 446.0, 204.0, 450.9, 0, 4.5))
    fr = fr.union(box(229.0, 446.0, 241.0, 450.9, 0, 4.5))
    return fr


def part_cubes():
    cubes = []
    cubes.append(letter_cube(87.3, 479.3, [("top", "E", 90), ("front", "R", 0),
                                           ("right", "A", 0), ("back", "R", -90), ("left", "E", 0),
                                           ("bottom", "A", 90)]))
    cubes.append(letter_cube(122.3, 479.3, [("top", "R", 90), ("front", "E", 90),
                                            ("right", "E", 0), ("back", "A", 90), ("left", "A", 0),
                                            ("bottom", "R", -90)]))
    cubes.append(letter_cube(157.5, 479.3, [("top", "A", 90), ("front", "R", 90),
                                            ("right", "A", 180), ("back", "R", 180), ("left", "R", 0),
                                            ("bottom", "E", 180)]))
    return cubes


parts = [
    part_twist_key(),
    part_window_key(),
    part_tall_clip(),
    part_u_frame(),
    part_cradle_box(),
    part_tall_fork(),
    arm_part(False, 16.7, 330.3),
    arm_part(True, 61.9, 450.5),
    part_frame(),
    part_l_wall(),
    part_small_gear_lever(),
    part_big_gear_lever(),
    part_slide_frame(),
] + part_cubes()

solids = []
for p in parts:
    for s in p.solids().vals():
        solids.append(s)

result = cq.Workplane("XY").newObject([cq.Compound.makeCompound(solids)])

VIEW = {"azimuth": 45, "elevation": 26}
